import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 60.0            # block height (Z)
W = 35.7            # overall width of the front band (X)
DB = 6.2            # front band depth (Y)
XB = 9.15           # X of the block's -X face
D = 16.15           # total block depth (Y)
R_BLOCK = 0.5       # edge rounding of the block

# hollow rear box (open at the back, partly open at the bottom)
T_WALL = 1.0        # wall thickness of the +X wall and the top
XC0 = 15.5          # -X inner face of the cavity (thick -X wall)
YC0 = 2.2           # front inner face of the cavity
FLOOR_T = 0.9       # floor plate thickness
FLOOR_LIFT = 0.6    # floor plate is set back from the bottom face
FLOOR_X1 = 29.3     # floor plate ends here (open slot along the +X wall)
NOTCH_X1 = 18.8     # rear notch of the floor plate: x from XC0 to NOTCH_X1
NOTCH_Y0 = 13.2     # ... and y from NOTCH_Y0 to the rear

# "[" shaped main plate (YZ plane) with two lugs
PX0, PX1 = 10.9, 12.9
PZ = 17.3           # half height of the plate
LUG_Z = 10.4        # inner z of the lugs
PY_MID = -11.6      # front of the plate middle
PY_LUG = -16.3      # front of the lugs
R_LUG = 0.9         # rounding of the lug corners

# thin inner sheet (parallel to main plate)
TX0, TX1 = 8.6, 9.4

# wings (45 deg, two diverging blades)
WY0, WY1 = -11.1, DB    # Y extent of the wings
CO = 29.1           # outer surface line of main blade: z = CO - x
TW = 1.2            # main blade thickness
X_WCUT = 10.3       # main blade lower end (vertical cut)
TT = 0.8            # thin blade thickness
GAP_ROOT = 0.2      # gap between the blades at the root
GAP_TIP = 0.9       # gap between the blades at the tip
XT = -5.6           # x of the outer tip corner
TIP_SLANT = 0.2    # dx/dz of the (slightly slanted) tip cut
WEB_D = 1.5         # length of the web joining the blades at the rear

# curved boss between plate and band face
BOSS_D = 2.25       # depth of boss at the plate
BOSS_X1 = W - R_BLOCK - 0.05   # x where the boss blends into the band face

# catch tab on the -X side
TAB_X0 = 0.5
TAB_ZT, TAB_ZB = 8.2, -8.0
TAB_Y0, TAB_Y1 = -4.9, -2.1
R_TAB_OUT = 0.6     # outer corner rounding of the tab
R_TAB_IN = 1.0      # blend radius between tab and thin sheet

# relief slots in the wedges above / below the wings
SLOTS = [(27.3, 2.0, -1.0), (23.7, 2.2, -1.0)]   # (z centre, height, x start)
SLOT_X1 = 8.8

# lettering
TEXT = "SENKU"
FONT = 13.3         # font size (cap height ~10 mm)
TEXT_SQUEEZE = 0.84 # condensed letter width
TEXT_DRAFT = 10.0   # draft angle of the letter cut (deg)
TXT_X_POS = (8.66, 0.18)    # (y, z) of the text on the +X face

S2 = math.sqrt(2.0)

# ---------------- block ----------------
band = cq.Workplane("XY").box(W, DB, H, centered=False).translate((0, 0, -H / 2))
rear = (cq.Workplane("XY").box(W - XB, D - DB, H, centered=False)
        .translate((XB, DB, -H / 2)))
block = band.union(rear)
block = block.edges("|Z or |X or |Y").fillet(R_BLOCK)

# open the band left of the block between the wings: only wedges remain
wedge_cut = (cq.Workplane("XZ", origin=(0, -1.0, 0))
             .polyline([(-1.0, CO + 1.0), (XB, CO - XB), (XB, -(CO - XB)),
                        (-1.0, -(CO + 1.0))]).close()
             .extrude(-(DB + 2.0)))
block = block.cut(wedge_cut)

# relief slots (through the wedges in Y), mirrored top / bottom
for zc, hs, xs in SLOTS:
    for sgn in (1, -1):
        slot = (cq.Workplane("XZ", origin=(0, -1.0, 0))
                .center((SLOT_X1 + xs) / 2, sgn * zc)
                .slot2D(SLOT_X1 - xs, hs)
                .extrude(-(DB + 2.0)))
        block = block.cut(slot)

# hollow rear box: open at the back and at the bottom ...
cav = (cq.Workplane("XY")
       .box(W - T_WALL - XC0, D - YC0 + 1.0, H - T_WALL + 1.0, centered=False)
       .translate((XC0, YC0, -H / 2 - 1.0)))
block = block.cut(cav)
# ... with a floor plate that leaves a slot along the +X wall
floor = (cq.Workplane("XY")
         .box(FLOOR_X1 - XC0 + 0.1, D - YC0 + 0.1, FLOOR_T, centered=False)
         .translate((XC0 - 0.1, YC0 - 0.1, -H / 2 + FLOOR_LIFT)))
notch = (cq.Workplane("XY")
         .box(NOTCH_X1 - XC0 + 1.0, D - NOTCH_Y0 + 1.0, FLOOR_T + 2, centered=False)
         .translate((XC0 - 1.0, NOTCH_Y0, -H / 2)))
floor = floor.cut(notch)
block = block.union(floor)

# ---------------- curved boss ----------------
Rb = ((BOSS_X1 - PX1) ** 2 + BOSS_D ** 2) / (2 * BOSS_D)
xm = (PX1 + BOSS_X1) / 2
ym = -Rb + math.sqrt(Rb ** 2 - (xm - BOSS_X1) ** 2)
boss = (cq.Workplane("XY").workplane(offset=-PZ)
        .moveTo(PX0, 0.5).lineTo(PX0, -BOSS_D).lineTo(PX1, -BOSS_D)
        .threePointArc((xm, ym), (BOSS_X1, 0.0))
        .lineTo(BOSS_X1, 0.5).close()
        .extrude(2 * PZ))


# ---------------- "[" plates ----------------
def bracket_plate(x0, x1, zt):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline([(0.5, -zt), (PY_LUG, -zt), (PY_LUG, -LUG_Z),
                       (PY_MID, -LUG_Z), (PY_MID, LUG_Z), (PY_LUG, LUG_Z),
                       (PY_LUG, zt), (0.5, zt)]).close()
            .extrude(x1 - x0))


main_plate = bracket_plate(PX0, PX1, PZ)
try:
    main_plate = (main_plate.edges("|X")
                  .edges(cq.selectors.BoxSelector((PX0 - 1, PY_LUG - 1, -PZ - 1),
                                                  (PX1 + 1, -0.2, PZ + 1)))
                  .fillet(R_LUG))
except Exception:
    pass
thin_plate = bracket_plate(TX0, TX1, CO - TW * S2 - GAP_ROOT * S2 - TX1)
# the middle part of the two plates is solid between them
filler = (cq.Workplane("XY")
          .box(PX0 - TX1 + 0.02, -PY_MID + 0.5, 2 * LUG_Z, centered=False)
          .translate((TX1 - 0.01, PY_MID, -LUG_Z)))

# ---------------- wings ----------------
CI = CO - TW * S2                       # inner line of main blade: z = CI - x
Z_TIP = CO - XT                         # z of the outer tip corner


def tip_x(z):
    """x on the slanted tip cut at height z"""
    return XT - (Z_TIP - z) * TIP_SLANT


def line_hit(z_of_x):
    """intersection of a blade line z(x) with the tip cut"""
    x = XT
    for _ in range(40):
        x = tip_x(z_of_x(x))
    return x, z_of_x(x)


# thin blade lines, diverging from the main blade towards the tip
def thin_line(offset_root, offset_tip):
    z_r = CI - offset_root * S2 - TX1
    z_t = CI - offset_tip * S2 - XT
    k = (z_t - z_r) / (XT - TX1)
    return lambda x: z_r + k * (x - TX1)


L_to = thin_line(GAP_ROOT, GAP_TIP)
L_ti = thin_line(GAP_ROOT + TT, GAP_TIP + TT)


def wing_main(sgn):
    p1 = line_hit(lambda x: CO - x)
    p2 = line_hit(lambda x: CI - x)
    pts = [(X_WCUT, CO - X_WCUT), p1, p2, (X_WCUT, CI - X_WCUT)]
    pts = [(x, sgn * z) for x, z in pts]
    return (cq.Workplane("XZ", origin=(0, WY0, 0)).polyline(pts).close()
            .extrude(-(WY1 - WY0)))


def wing_thin(sgn):
    zo = L_to(TX1)
    zi = L_ti(TX0)
    pts = [(TX1, zo), line_hit(L_to), line_hit(L_ti), (TX0, zi),
           (TX0, zi - 0.6), (TX1, zi - 0.6)]
    pts = [(x, sgn * z) for x, z in pts]
    return (cq.Workplane("XZ", origin=(0, WY0, 0)).polyline(pts).close()
            .extrude(-(WY1 - WY0)))


def wing_web(sgn):
    """closes the gap between the two blades at their rear end"""
    pts = [(TX1, CI - TX1), line_hit(lambda x: CI - x), line_hit(L_to),
           (TX1, L_to(TX1))]
    pts = [(x, sgn * z) for x, z in pts]
    return (cq.Workplane("XZ", origin=(0, WY1 - WEB_D, 0)).polyline(pts).close()
            .extrude(-WEB_D))


wings = wing_main(1).union(wing_main(-1)).union(wing_thin(1)).union(wing_thin(-1))
wings = wings.union(wing_web(1)).union(wing_web(-1))

# ---------------- tab ----------------
# XZ profile: rounded outer corners, concave blend into the thin sheet
c45 = math.sqrt(0.5)
tab = (cq.Workplane("XZ", origin=(0, TAB_Y0, 0))
       .moveTo(TX0 + 0.4, TAB_ZT + R_TAB_IN)
       .lineTo(TX0, TAB_ZT + R_TAB_IN)
       .threePointArc((TX0 - R_TAB_IN * (1 - c45), TAB_ZT + R_TAB_IN * (1 - c45)),
                      (TX0 - R_TAB_IN, TAB_ZT))
       .lineTo(TAB_X0 + R_TAB_OUT, TAB_ZT)
       .threePointArc((TAB_X0 + R_TAB_OUT * (1 - c45), TAB_ZT - R_TAB_OUT * (1 - c45)),
                      (TAB_X0, TAB_ZT - R_TAB_OUT))
       .lineTo(TAB_X0, TAB_ZB + R_TAB_OUT)
       .threePointArc((TAB_X0 + R_TAB_OUT * (1 - c45), TAB_ZB + R_TAB_OUT * (1 - c45)),
                      (TAB_X0 + R_TAB_OUT, TAB_ZB))
       .lineTo(TX0 - R_TAB_IN, TAB_ZB)
       .threePointArc((TX0 - R_TAB_IN * (1 - c45), TAB_ZB - R_TAB_IN * (1 - c45)),
                      (TX0, TAB_ZB - R_TAB_IN))
       .lineTo(TX0 + 0.4, TAB_ZB - R_TAB_IN)
       .close()
       .extrude(-(TAB_Y1 - TAB_Y0)))

# ---------------- assemble ----------------
part = (block.union(boss).union(main_plate).union(thin_plate).union(filler)
        .union(wings).union(tab))

# ---------------- lettering cut through the thin +X wall ----------------
# reads top to bottom, letter tops toward +Y; slight draft on the cut
flat = cq.Compound.makeText(TEXT, FONT, 0, halign="center", valign="center")
letters = [cq.Solid.extrudeLinear(f, cq.Vector(0, 0, -(T_WALL + 0.25)), TEXT_DRAFT)
           for f in flat.Faces()]
txt = cq.Compound.makeCompound(letters).transformGeometry(
    cq.Matrix([[0, 0, 1, W + 0.05],
               [0, 1, 0, TXT_X_POS[0]],
               [-TEXT_SQUEEZE, 0, 0, TXT_X_POS[1]]]))
part = part.cut(cq.Workplane("XY").add(txt))

result = part
